"""Equal pipe tee with raised longitudinal seam beads.

Run along Y, branch along +X, branch axis in the XY plane (Z up).
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
OD = 100.0             # outside diameter of run and branch (equal tee)
WALL = 3.7             # wall thickness
RUN_POS = 116.5        # run: centre-to-end towards +Y
RUN_NEG = 112.5        # run: centre-to-end towards -Y
C_BRANCH = 116.5       # branch: centre-to-end along +X
FILLET_R = 4.0         # blend radius at the outside run/branch intersection
END_ROUND = 0.8        # small round on the pipe end edges

RIB_D = 3.2            # diameter of the raised seam beads (round rods, domed ends)
RIB_PROUD = 1.4        # how far a bead stands proud of the pipe surface
TOP_RIB_ANG = 2.2      # top bead sits this many degrees round towards -X
BOT_RIB_ANG = 1.6      # bottom bead sits this many degrees round towards +X

# bead tip positions: along Y measured from the branch axis, along X from the run axis
TOP_RIB = (-107.0, 113.0)       # top of the run
BOT_RIB = (-106.5, 110.5)       # underside of the run
LEFT_RIB = (-106.5, 110.5)      # -X side of the run
SIDE_RIB_IN = 54.0              # +X side beads stop just short of the branch blend
SIDE_RIB_NEG_OUT = 106.3
SIDE_RIB_POS_OUT = 110.3
BR_RIB = (65.0, 110.0)          # branch top / bottom beads

# angular position of the cylinder seams (kept out of sight / away from the crotch).
# The first pair that gives a clean blend is used.
SEAM_CANDIDATES = [(-89.0, -90.0), (180.0, 0.0), (0.0, 90.0), (-91.5, 0.0), (90.0, -90.0)]
RUN_BORE_SEAM_ROT = 45.0        # bore seams on the faces no standard view looks at
BRANCH_BORE_SEAM_ROT = 90.0

R = OD / 2.0
RI = R - WALL


# ---------------- helpers ----------------
def cyl_y(radius, y0, y1, seam_rot):
    """solid cylinder on the Y axis from y0 to y1; seam turned seam_rot deg about Y"""
    c = cq.Solid.makeCylinder(radius, y1 - y0, cq.Vector(0, y0, 0), cq.Vector(0, 1, 0))
    return cq.Workplane("XY").add(c).rotate((0, 0, 0), (0, 1, 0), seam_rot)


def cyl_x(radius, x0, x1, seam_rot):
    """solid cylinder on the X axis from x0 to x1; seam turned seam_rot deg about X"""
    c = cq.Solid.makeCylinder(radius, x1 - x0, cq.Vector(x0, 0, 0), cq.Vector(1, 0, 0))
    return cq.Workplane("XY").add(c).rotate((0, 0, 0), (1, 0, 0), seam_rot)


def capsule(t0, t1, d):
    """round rod with hemispherical ends; t0 and t1 are the tips of the rod"""
    t0 = cq.Vector(*t0)
    t1 = cq.Vector(*t1)
    r = d / 2.0
    u = (t1 - t0).normalized()
    p0 = t0 + u * r
    p1 = t1 - u * r
    rod = cq.Solid.makeCylinder(r, (p1 - p0).Length, p0, u)
    s0 = cq.Solid.makeSphere(r, p0, angleDegrees1=-90, angleDegrees2=90)
    s1 = cq.Solid.makeSphere(r, p1, angleDegrees1=-90, angleDegrees2=90)
    return (cq.Workplane("XY").add(rod)
            .union(cq.Workplane("XY").add(s0))
            .union(cq.Workplane("XY").add(s1)))


def is_clean(wp, vmin):
    try:
        solids = wp.solids().vals()
        return (len(solids) == 1 and solids[0].isValid() and solids[0].Volume() > vmin)
    except Exception:
        return False


# approximate shell volume, used only to sanity-check the boolean results
V_EXPECT = (math.pi * (R * R - RI * RI) * (RUN_POS + RUN_NEG)
            + math.pi * (R * R - RI * RI) * (C_BRANCH - R))


# ---------------- seam beads ----------------
rc = R + RIB_PROUD - RIB_D / 2.0          # radius of the bead centre lines


def run_bead(ang_deg, y0, y1):
    """bead along the run; angle measured from +Z towards +X"""
    a = math.radians(ang_deg)
    x, z = rc * math.sin(a), rc * math.cos(a)
    return capsule((x, y0, z), (x, y1, z), RIB_D)


def branch_bead(z_sign, x0, x1):
    return capsule((x0, 0, z_sign * rc), (x1, 0, z_sign * rc), RIB_D)


def make_beads():
    return [
        run_bead(-TOP_RIB_ANG, *TOP_RIB),                       # top of run
        run_bead(180.0 - BOT_RIB_ANG, *BOT_RIB),                # underside of run
        run_bead(-90.0, *LEFT_RIB),                             # -X side of run
        run_bead(90.0, SIDE_RIB_IN, SIDE_RIB_POS_OUT),          # +X side, +Y half
        run_bead(90.0, -SIDE_RIB_NEG_OUT, -SIDE_RIB_IN),        # +X side, -Y half
        branch_bead(1, *BR_RIB),                                # branch top
        branch_bead(-1, *BR_RIB),                               # branch underside
    ]


# ---------------- body ----------------
def build(run_seam, branch_seam, blend=True, end_round=True):
    outer = cyl_y(R, -RUN_NEG, RUN_POS, run_seam).union(
        cyl_x(R, 0, C_BRANCH, branch_seam))
    if blend:
        outer = outer.edges("%ELLIPSE").fillet(FILLET_R)

    bore = cyl_y(RI, -RUN_NEG - 1, RUN_POS + 1, RUN_BORE_SEAM_ROT).union(
        cyl_x(RI, 0, C_BRANCH + 1, BRANCH_BORE_SEAM_ROT))
    body = outer.cut(bore)

    if end_round:
        # round the outer and inner circular edges of the three pipe ends
        ends = (cq.selectors.BoxSelector((-R - 1, RUN_POS - 0.1, -R - 1),
                                         (R + 1, RUN_POS + 0.1, R + 1))
                + cq.selectors.BoxSelector((-R - 1, -RUN_NEG - 0.1, -R - 1),
                                           (R + 1, -RUN_NEG + 0.1, R + 1))
                + cq.selectors.BoxSelector((C_BRANCH - 0.1, -R - 1, -R - 1),
                                           (C_BRANCH + 0.1, R + 1, R + 1)))
        body = body.edges(ends).fillet(END_ROUND)

    for b in make_beads():
        body = body.union(b)
    return body


result = None
for blend, end_round in ((True, True), (True, False), (False, True), (False, False)):
    for rs, bs in SEAM_CANDIDATES:
        try:
            cand = build(rs, bs, blend, end_round)
        except Exception:
            continue
        if is_clean(cand, 0.9 * V_EXPECT):
            result = cand
            break
    if result is not None:
        break

if result is None:      # last resort: plain booleans, no blends
    result = build(0.0, 0.0, blend=False, end_round=False)

VIEW = {"azimuth": 45, "elevation": 26}
